import cadquery as cq

# Driving dimensions (mm)
LENGTH = 200.0      # X  (plate length)
WIDTH = 120.0       # Y  (plate width)
THICK = 20.0        # Z  (plate thickness)
HOLE_D = 10.0       # through-hole diameter
PITCH_X = 30.0      # hole pitch along X
PITCH_Y = 30.0      # hole pitch along Y
N_X = 5             # columns
N_Y = 3             # rows
FIRST_X_FROM_LEFT = 30.0   # first column centre measured from the -X edge
SEAM_ANGLE = -90.0  # angular position of the cylindrical-face seam of each hole

# Base plate, bottom face on Z=0
plate = cq.Workplane("XY").box(LENGTH, WIDTH, THICK, centered=(True, True, False))

# Hole grid (offset toward -X, centred in Y)
x0 = -LENGTH / 2 + FIRST_X_FROM_LEFT
pts = [
    (x0 + i * PITCH_X, (j - (N_Y - 1) / 2) * PITCH_Y)
    for i in range(N_X)
    for j in range(N_Y)
]

# One drill body, bored upward through the plate, seam rotated to SEAM_ANGLE
drill = cq.Solid.makeCylinder(
    HOLE_D / 2, THICK + 2.0, cq.Vector(0, 0, -1.0), cq.Vector(0, 0, 1)
).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)

cutters = cq.Workplane("XY")
for (x, y) in pts:
    cutters = cutters.add(drill.translate(cq.Vector(x, y, 0)))

result = plate.cut(cutters)

VIEW = {"azimuth": 45, "elevation": 26}
